"""Crown-topped turned piece (chess-queen like).

Revolved body: flat underside with a conical bevel, a straight conical body that
runs tangentially into one large concave arc forming the waist and the flared
crown.  The crown top is a narrow flat rim ring with a conical dish inside.
Eight V notches (four through-cuts across the crown) leave eight pointed tips
with small flat tops; a ball sits in the centre of the dish.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
H_TOP = 95.0          # overall height (top of the crown tips)
R_BOTTOM = 19.08      # radius of the flat underside
R_BASE = 22.2         # widest radius (top of the base bevel)
H_BEVEL = 5.84        # height of the base bevel
CONE_SLOPE = 0.23     # dr/dh of the straight conical body (radius shrinks upward)
NECK_R = 9.52         # narrowest radius of the waist
FLARE_RAD = 57.2      # radius of the concave arc forming waist + crown flare
R_FLAT_IN = 14.5      # inner radius of the flat rim ring on the crown
DISH_ANGLE = 37.4     # slope of the conical dish inside the crown (deg from horizontal)

N_POINTS = 8          # number of crown points
H_VALLEY = 86.6       # height of the V-notch bottoms
V_HALF = 30.0         # half angle of the V notches (deg)

R_BALL = 8.7          # centre ball radius
H_BALL_TOP = 92.1     # height of the top of the centre ball

# ---------------- derived profile geometry ----------------
k = CONE_SLOPE
C = R_BASE + k * H_BEVEL                              # cone line: r = C - k*h
a = NECK_R + FLARE_RAD                                # arc centre radius (outside the part)
b = (FLARE_RAD * math.sqrt(1 + k * k) + C - a) / k    # arc centre height (arc tangent to cone)
h_t = b - FLARE_RAD * k / math.sqrt(1 + k * k)        # cone / arc tangent point
r_t = C - k * h_t
R_TOP = a - math.sqrt(FLARE_RAD ** 2 - (H_TOP - b) ** 2)   # crown rim radius

h_m = 0.5 * (h_t + H_TOP)                             # a point on the arc for threePointArc
r_m = a - math.sqrt(FLARE_RAD ** 2 - (h_m - b) ** 2)

h_dish_axis = H_TOP - R_FLAT_IN * math.tan(math.radians(DISH_ANGLE))

# ---------------- revolved body ----------------
profile = (
    cq.Workplane("XZ")
    .moveTo(0, 0)
    .lineTo(R_BOTTOM, 0)                    # underside
    .lineTo(R_BASE, H_BEVEL)                # base bevel
    .lineTo(r_t, h_t)                       # straight conical body
    .threePointArc((r_m, h_m), (R_TOP, H_TOP))   # waist + crown flare (tangent to the cone)
    .lineTo(R_FLAT_IN, H_TOP)               # flat rim ring
    .lineTo(0, h_dish_axis)                 # conical dish
    .close()
)
body = profile.revolve(360, (0, 0, 0), (0, 1, 0))

# ---------------- V notches: through-cuts across the crown ----------------
reach = 2.5 * R_BASE
tan_v = math.tan(math.radians(V_HALF))
for i in range(N_POINTS // 2):
    notch = (
        cq.Workplane("YZ")
        .polyline([(0, H_VALLEY),
                   (reach * tan_v, H_VALLEY + reach),
                   (-reach * tan_v, H_VALLEY + reach)])
        .close()
        .extrude(reach, both=True)                       # V prism along X, through both sides
        .rotate((0, 0, 0), (0, 0, 1), i * 360.0 / N_POINTS)
    )
    body = body.cut(notch)

# ---------------- centre ball ----------------
ball = (
    cq.Workplane("XY")
    .sphere(R_BALL)
    .rotate((0, 0, 0), (0, 1, 0), 90)       # poles/seam end up buried inside the body
    .translate((0, 0, H_BALL_TOP - R_BALL))
)

# valleys on the 45-degree lines, tips at 22.5 + k*45 degrees (rotation keeps the
# 8-fold pattern and moves the revolve seam onto a valley line)
result = body.union(ball).rotate((0, 0, 0), (0, 0, 1), 45)

VIEW = {"azimuth": 45, "elevation": 26}
